import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # overall flange length (X)
W = 81.6           # flange width (Z) = diameter of central flange arc
S = 100.0          # bolt-hole spacing
R_EAR = (L - S) / 2.0   # ear radius
D_HOLE = 10.2      # bolt hole diameter
T = 1.3            # flange thickness (Y)

D_CUP = 54.5       # housing (cup) outer diameter
H = 22.0           # total depth: flange front face -> cup back face
R_BASE = 5.0       # fillet between flange back face and cup wall
R_TOP = 5.5        # rounded back edge of the cup

D_REC = 50.4       # shallow recess on the flange front face
REC_DEPTH = 3.6
R_REC_RIM = 0.5    # small round on the recess rim

D_OPEN = 35.0      # diameter of the spherical seat opening on the cup back face
R_DISH = 17.5      # spherical radius of the seat (hemispherical when = D_OPEN/2)
R_LIP = 0.4        # round on the dish rim

SEAM_ANGLE = 110.0  # where the revolve seam sits (cosmetic only)

VIEW = {"azimuth": 45, "elevation": 26}


def flange_outline():
    """Two-ear flange outline in the XZ plane (local x = X, local y = Z)."""
    R = W / 2.0
    c = S / 2.0
    cphi = (R - R_EAR) / c
    sphi = math.sqrt(1.0 - cphi * cphi)
    # tangent points (right side, upper)
    t1 = (R * cphi, R * sphi)
    t2 = (c + R_EAR * cphi, R_EAR * sphi)
    wp = (
        cq.Workplane("XZ")
        .moveTo(t1[0], t1[1])
        .lineTo(t2[0], t2[1])
        .threePointArc((c + R_EAR, 0.0), (t2[0], -t2[1]))
        .lineTo(t1[0], -t1[1])
        .threePointArc((0.0, -R), (-t1[0], -t1[1]))
        .lineTo(-t2[0], -t2[1])
        .threePointArc((-c - R_EAR, 0.0), (-t2[0], t2[1]))
        .lineTo(-t1[0], t1[1])
        .threePointArc((0.0, R), (t1[0], t1[1]))
        .close()
    )
    return wp


# flange plate: front face at Y=0, back face at Y=T
flange = flange_outline().extrude(-T)

# ---- cup body: revolved profile (x = radius, y = axial) around the Y axis ----
rc = D_CUP / 2.0
ro = D_OPEN / 2.0
zc = math.sqrt(max(R_DISH ** 2 - ro ** 2, 0.0))       # dish sphere centre above back face
dish_depth = R_DISH - zc
s45 = math.sin(math.pi / 4)

prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(rc, 0)
    .lineTo(rc, H - R_TOP)
    .threePointArc(
        (rc - R_TOP + R_TOP * s45, H - R_TOP + R_TOP * s45),
        (rc - R_TOP, H),
    )
    .lineTo(ro, H)
    .threePointArc(
        (R_DISH * math.sin(0.5 * math.asin(ro / R_DISH)),
         H + zc - R_DISH * math.cos(0.5 * math.asin(ro / R_DISH))),
        (0, H - dish_depth),
    )
    .close()
)
cup = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)

body = flange.union(cup)

# fillet at the cup base (circle of radius rc on the flange back face)
body = body.edges(
    cq.selectors.BoxSelector((-rc - 0.5, T - 0.2, -rc - 0.5), (rc + 0.5, T + 0.2, rc + 0.5), boundingbox=True)
).fillet(R_BASE)

# round on the dish rim
body = body.edges(
    cq.selectors.BoxSelector((-ro - 0.3, H - 0.2, -ro - 0.3), (ro + 0.3, H + 0.2, ro + 0.3), boundingbox=True)
).fillet(R_LIP)

# bolt holes
body = body.cut(
    cq.Workplane("XZ")
    .pushPoints([(-S / 2.0, 0), (S / 2.0, 0)])
    .circle(D_HOLE / 2.0)
    .extrude(-T * 3)
    .translate((0, -T, 0))
)

# shallow recess on the front face
rr = D_REC / 2.0
body = body.cut(
    cq.Workplane("XZ").circle(rr).extrude(-REC_DEPTH)
)
body = body.edges(
    cq.selectors.BoxSelector((-rr - 0.3, -0.2, -rr - 0.3), (rr + 0.3, 0.2, rr + 0.3), boundingbox=True)
).fillet(R_REC_RIM)

result = body
